import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_TOP = 50.0        # outer radius at the rim
R_BOT = 28.9        # outer radius at the foot
R_MID = 33.4        # outer radius at half height (sets the flare curvature)
H = 52.7            # overall height
T = 2.9             # wall thickness (normal to the flared surface)
FLANGE_R_IN = 22.2  # bore radius of the inward lip at the foot
FLANGE_T = 1.85     # thickness of that lip
BOSS_POS = 40.7     # radial position of the two bosses (on the X axis)
BOSS_R = 7.5        # boss outer radius
BORE_R = 3.75       # bore radius through each boss

# ---------------- flare arc (circle through foot, mid and rim points) --------
ZM = 0.5 * H


def _circle_centre(p1, p2, p3):
    (x1, y1), (x2, y2), (x3, y3) = p1, p2, p3
    d = 2.0 * (x1 * (y2 - y3) + x2 * (y3 - y1) + x3 * (y1 - y2))
    ux = ((x1 ** 2 + y1 ** 2) * (y2 - y3) + (x2 ** 2 + y2 ** 2) * (y3 - y1)
          + (x3 ** 2 + y3 ** 2) * (y1 - y2)) / d
    uy = ((x1 ** 2 + y1 ** 2) * (x3 - x2) + (x2 ** 2 + y2 ** 2) * (x1 - x3)
          + (x3 ** 2 + y3 ** 2) * (x2 - x1)) / d
    return ux, uy


CX, CZ = _circle_centre((R_BOT, 0.0), (R_MID, ZM), (R_TOP, H))
R_ARC = math.hypot(R_BOT - CX, 0.0 - CZ)


def r_at(z, off):
    """radius at height z of the flared surface offset inward by `off`"""
    return CX - math.sqrt((R_ARC + off) ** 2 - (z - CZ) ** 2)


def envelope(off, z0=0.0, z1=H, seam_deg=0.0):
    """solid of revolution bounded by the flared surface offset by `off`"""
    prof = (
        cq.Workplane("XZ")
        .moveTo(0, z0)
        .lineTo(r_at(z0, off), z0)
        .threePointArc((r_at(ZM, off), ZM), (r_at(H, off), H))
    )
    if z1 > H:
        prof = prof.lineTo(r_at(H, off), z1)
    prof = prof.lineTo(0, z1).close()
    return prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate(
        (0, 0, 0), (0, 0, 1), seam_deg
    )


# ---------------- flared shell ----------------
outer = envelope(0.0, seam_deg=180.0)          # outer skin, seam at -X
inner = envelope(T, z0=FLANGE_T, z1=H + 1.0)   # inner void, seam under +X boss
foot_bore = (
    cq.Workplane("XY").workplane(offset=-1).circle(FLANGE_R_IN).extrude(H + 2)
)
body = outer.cut(inner).cut(foot_bore)

# ---------------- bosses ----------------
mid_wall = envelope(0.5 * T)  # trims the bosses inside the wall thickness
bosses = (
    cq.Workplane("XY")
    .pushPoints([(BOSS_POS, 0), (-BOSS_POS, 0)])
    .circle(BOSS_R)
    .extrude(H)
    .intersect(mid_wall)
)
body = body.union(bosses)

# bores straight down through boss and flared wall
bores = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .pushPoints([(BOSS_POS, 0), (-BOSS_POS, 0)])
    .circle(BORE_R)
    .extrude(H + 2)
)
result = body.cut(bores).clean()

VIEW = {"azimuth": 45, "elevation": 26}
